import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Pair of mirrored, kite-shaped funnel frames (vent / trim bezels).
# Each frame: straight inner rail (">" shaped inner face) along Y, outer
# edge with a rounded vertex about one third from the back, a funnel-shaped
# through-opening (gentle band, steep band, throat, bevel underneath), a
# leaning outer wall and a sloped underside.  The front part droops slightly
# towards the front tip.  Built from ruled lofts + boolean cuts, then
# mirrored about the YZ plane.
# Units: mm.  +Y = back, -Y = front, Z up, top at z = 0.
# ---------------------------------------------------------------------------

L = 236.0                 # overall length (Y)
Y_F = -L / 2.0            # front tip
Y_B = L / 2.0             # back tip

X_IN_TOP = 20.5           # inner edge, top corner
X_IN_APEX = (16.2, 13.5, 17.3)   # inner face apex: front / middle / back
X_IN_BOT = 23.4           # inner edge, bottom corner
X_OPEN = 24.0             # opening-side wall of the inner rail

Z_MID = -8.5              # outer wall height / inner face apex depth
H = 18.5                  # total depth
LEAN = (1.2, 3.5)         # outer wall lean (top inset): back / front rail
RIM = 0.8                 # flat rim between the outer ridge and the funnel

DROOP_TOP = 3.0           # top drop at the front tip
DROOP_STEP = 0.8          # small step in the top where the droop starts
DROOP_MID = 2.8           # drop of the outer-wall foot at the front tip
Y_DROOP = 22.0            # droop starts here (towards the front)

# outer outline at z = Z_MID (max plan extent), back tip -> vertex
BACK_OUT = [(22.3, Y_B), (28.6, 109.3), (35.4, 99.3), (47.3, 84.0),
            (58.2, 69.5), (65.0, 59.6), (72.7, 44.6), (77.3, 35.5)]
# vertex -> front tip
FRONT_OUT = [(77.3, 35.5), (75.8, 19.8), (69.3, 0.0), (57.5, -40.9),
             (37.9, -89.6), (26.5, Y_F)]
TIP_TOP_W = 1.2           # width of the (almost pointed) tips at the top

# funnel: transition line, throat and bevel underneath
Z_B = -5.0                # depth of the light/dark transition line
Z_C = -15.0               # throat (narrowest section of the opening)
BEVEL = 2.5               # underside bevel around the opening (plan width)
OB_BACK = [(X_OPEN, 89.8), (33.0, 79.8), (42.7, 66.3), (52.3, 51.0), (61.5, 34.0)]
OB_FRONT = [(61.5, 34.0), (54.3, 0.0), (41.4, -39.8), (34.1, -59.7), (X_OPEN, -84.0)]
OC_BACK = [(X_OPEN, 68.5), (33.0, 58.6), (40.8, 47.0), (46.5, 35.5), (47.5, 31.0)]
OC_FRONT = [(47.5, 31.0), (42.5, 9.0), (X_OPEN, -55.6)]
OE_Y = (-56.0, 70.5)      # bevel ends along the inner rail (front, back)


# ---------------------------------------------------------------------------
# small 2D helpers
# ---------------------------------------------------------------------------
def _norm(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def _inward(a, b):
    d = _norm((b[0] - a[0], b[1] - a[1]))
    return (d[1], -d[0])


def offset_curves(back, front, d):
    """Offset a (back: tip->vertex, front: vertex->tip) curve pair towards
    the inside (negative = outwards).  d = value or (d_back, d_front)."""
    db, df = d if isinstance(d, tuple) else (d, d)
    nb = []
    n = len(back)
    for i in range(n - 1):
        nn = _inward(back[max(i - 1, 0)], back[min(i + 1, n - 1)])
        nb.append((back[i][0] + db * nn[0], back[i][1] + db * nn[1]))
    # vertex: intersection of the two offset tangent lines
    n1 = _inward(back[-2], back[-1])
    n2 = _inward(front[0], front[1])
    c = n1[0] * n2[0] + n1[1] * n2[1]
    a = (db - c * df) / (1.0 - c * c)
    b = (df - c * db) / (1.0 - c * c)
    vtx = (back[-1][0] + a * n1[0] + b * n2[0], back[-1][1] + a * n1[1] + b * n2[1])
    nb.append(vtx)
    nf = [vtx]
    m = len(front)
    for i in range(1, m):
        nn = _inward(front[i - 1], front[min(i + 1, m - 1)])
        nf.append((front[i][0] + df * nn[0], front[i][1] + df * nn[1]))
    return nb, nf


def _hit_x(a, b, x):
    t = (x - a[0]) / (b[0] - a[0])
    return (x, a[1] + t * (b[1] - a[1]))


def start_on_x(pts, x):
    """Trim or extend the start of a polyline so it begins on X = x."""
    for i in range(len(pts) - 1):
        a, b = pts[i], pts[i + 1]
        if (a[0] - x) * (b[0] - x) <= 0 and a[0] != b[0]:
            p = _hit_x(a, b, x)
            rest = pts[i + 1:]
            if math.hypot(rest[0][0] - p[0], rest[0][1] - p[1]) < 2.0 and len(rest) > 1:
                rest = rest[1:]
            return [p] + rest
    return [_hit_x(pts[0], pts[1], x)] + pts[1:]


def end_on_x(pts, x):
    return list(reversed(start_on_x(list(reversed(pts)), x)))


def circle3(a, m, b):
    """centre and radius of the circle through three 2D points"""
    ax, ay = a
    bx, by = m
    cx, cy = b
    d = 2.0 * (ax * (by - cy) + bx * (cy - ay) + cx * (ay - by))
    ux = ((ax * ax + ay * ay) * (by - cy) + (bx * bx + by * by) * (cy - ay)
          + (cx * cx + cy * cy) * (ay - by)) / d
    uy = ((ax * ax + ay * ay) * (cx - bx) + (bx * bx + by * by) * (ax - cx)
          + (cx * cx + cy * cy) * (bx - ax)) / d
    return (ux, uy), math.hypot(ax - ux, ay - uy)


def droop(y):
    return -DROOP_MID * (Y_DROOP - y) / (Y_DROOP - Y_F) if y < Y_DROOP else 0.0


# ---------------------------------------------------------------------------
# edge / wire helpers
# ---------------------------------------------------------------------------
def V(p, z):
    return cq.Vector(p[0], p[1], z)


def line(a, b, z):
    return cq.Edge.makeLine(V(a, z), V(b, z))


def curve(pts, z):
    if len(pts) == 2:
        return line(pts[0], pts[1], z)
    if len(pts) == 3:
        return cq.Edge.makeThreePointArc(V(pts[0], z), V(pts[1], z), V(pts[2], z))
    return cq.Edge.makeSpline([V(p, z) for p in pts])


def outline_wire(inner, z, back, front, y_f, y_b):
    """Planar 5-edge outline: inner edge, back tip, back-outer curve,
    front-outer curve, front tip."""
    p_fi, p_bi = (inner, y_f), (inner, y_b)
    edges = [line(p_fi, p_bi, z), line(p_bi, back[0], z), curve(back, z),
             curve(front, z), line(front[-1], p_fi, z)]
    return cq.Wire.assembleEdges(edges)


def mid_wire():
    """Outline at the outer-wall foot, lowered towards the front tip."""
    def P(p):
        return cq.Vector(p[0], p[1], Z_MID + droop(p[1]))

    fa, fm, fb = (X_IN_APEX[0], Y_F), (X_IN_APEX[1], -10.0), (X_IN_APEX[2], Y_B)
    (ux, uy), r = circle3(fa, fm, fb)
    inner_y = [Y_F, -75.0, -30.0, Y_DROOP, 70.0, Y_B]
    inner = [(ux - math.sqrt(r * r - (y - uy) ** 2), y) for y in inner_y]
    front = FRONT_OUT
    edges = [
        cq.Edge.makeSpline([P(p) for p in inner]),
        cq.Edge.makeLine(P(inner[-1]), P(BACK_OUT[0])),
        cq.Edge.makeSpline([P(p) for p in BACK_OUT]),
        cq.Edge.makeSpline([P(p) for p in front]),
        cq.Edge.makeLine(P(front[-1]), P(inner[0])),
    ]
    return cq.Wire.assembleEdges(edges)


def opening_wire(back, front, z):
    """3-edge opening outline: inner line, back curve, front curve."""
    edges = [line(front[-1], back[0], z), curve(back, z), curve(front, z)]
    return cq.Wire.assembleEdges(edges)


def bevel_curves(d, y_f, y_b):
    b, f = offset_curves(OC_BACK, OC_FRONT, -d)
    b = [(X_OPEN, y_b)] + b[1:]
    f = [f[0], f[1], (X_OPEN, y_f)] if len(f) == 3 else [f[0], (X_OPEN, y_f)]
    return b, f


def make_frame():
    # ---- solid body -------------------------------------------------------
    tb, tf = offset_curves(BACK_OUT, FRONT_OUT, LEAN)
    tb = [(X_IN_TOP + TIP_TOP_W, Y_B)] + tb[1:]
    tf = tf[:-1] + [(X_IN_TOP + TIP_TOP_W, Y_F)]
    w_top = outline_wire(X_IN_TOP, 0.0, tb, tf, Y_F, Y_B)

    w_mid = mid_wire()

    # deepest footprint: just outside the bevel around the opening
    y2f, y2b = OE_Y[0] - 1.0, OE_Y[1] + 2.0
    bb, bf = bevel_curves(BEVEL + 0.8, y2f, y2b)
    bb = [(X_OPEN + 1.5, y2b)] + bb[1:]
    bf = bf[:-1] + [(X_OPEN + 1.5, y2f)]
    w_bot = outline_wire(X_IN_BOT, -H, bb, bf, y2f, y2b)
    body = cq.Solid.makeLoft([w_top, w_mid, w_bot], True)

    # ---- funnel through-opening -------------------------------------------
    ab, af = offset_curves(BACK_OUT, FRONT_OUT, (LEAN[0] + RIM, LEAN[1] + RIM))
    ab = start_on_x(ab, X_OPEN)
    af = end_on_x(af, X_OPEN)
    o_a = opening_wire(ab, af, 0.0)
    o_b = opening_wire(OB_BACK, OB_FRONT, Z_B)
    o_c = opening_wire(OC_BACK, OC_FRONT, Z_C)
    eb, ef = bevel_curves(BEVEL, OE_Y[0], OE_Y[1])
    o_e = opening_wire(eb, ef, -H)
    k = (H + 4.0 + Z_C) / (H + Z_C)
    gb, gf = bevel_curves(BEVEL * k, OE_Y[0] - 3.0, OE_Y[1] + 3.0)
    o_g = opening_wire(gb, gf, -H - 4.0)

    cutter = cq.Solid.makeLoft(
        [opening_wire(ab, af, 4.0), o_a, o_b, o_c, o_e, o_g], True)

    part = body.cut(cutter)

    # ---- slight droop of the top towards the front tip --------------------
    far = 400.0
    slope = (DROOP_TOP - DROOP_STEP) / (Y_DROOP - Y_F)
    prof = [(Y_DROOP - far, -DROOP_STEP - slope * far), (Y_DROOP, -DROOP_STEP),
            (Y_DROOP, 60.0), (Y_DROOP - far, 60.0)]
    wedge = (cq.Workplane("YZ").polyline(prof).close()
             .extrude(150.0, both=True).val())
    part = part.cut(wedge)
    return cq.Workplane("XY").add(part)


right = make_frame()
left = right.mirror("YZ")

result = right.union(left)
